import math
import cadquery as cq

# =====================================================================
#  Comb / finger bar with star-shaped (octagon + 8 wedge slot) holes.
#  A flat bar carries a staggered row of star holes: N_CENTER on the
#  centre line and N_CENTER + 1 half-stars on each long edge.  Under the
#  middle of the bar every star is surrounded by slotted "fingers" that
#  hang down: each finger is the piece of the star's convex hull (a
#  16-gon) that lies between two neighbouring slots.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
L = 240.0          # overall length of the bar (X)
W = 23.0           # bar depth (Y)
T = 9.8            # top plate thickness
H = 44.5           # overall height (plate + fingers)
PITCH = 40.0       # spacing of the star holes along X
N_CENTER = 3       # star holes on the centre line (edge stars: N_CENTER + 1 per side)
N_SLOTS = 8        # radial slots per star
CORE_AF = 10.0     # across-flats of the octagonal core (corners point along the slots)
R_SLOT = 9.87      # distance from the star centre to the flat end of each slot
SLOT_ANGLE = 180.0 / (2 * N_SLOTS)   # half-angle of the wedge-shaped slots (deg)

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived values ----------------
_TAN = math.tan(math.radians(SLOT_ANGLE))
R_ROOT = CORE_AF / 2.0            # a slot wall meets the core flat at this radius
H_ROOT = R_ROOT * _TAN            # half width of a slot at the core
H2 = R_SLOT * _TAN                # half width of a slot at its outer end
DA = 2.0 * math.pi / N_SLOTS

# star centres: on the centre line and (staggered) on both long edges
centre_x = [(i - (N_CENTER - 1) / 2.0) * PITCH for i in range(N_CENTER)]
edge_x = [(i - N_CENTER / 2.0) * PITCH for i in range(N_CENTER + 1)]


def _pt(cx, cy, a, r, h):
    """point at radius r along direction a, offset h sideways (CCW positive)."""
    ca, sa = math.cos(a), math.sin(a)
    return (cx + r * ca - h * sa, cy + r * sa + h * ca)


def star_points(cx, cy):
    """Outline of one star hole: octagonal core + wedge-shaped radial slots."""
    pts = []
    for k in range(N_SLOTS):
        a = k * DA
        pts.append(_pt(cx, cy, a, R_ROOT, -H_ROOT))
        pts.append(_pt(cx, cy, a, R_SLOT, -H2))
        pts.append(_pt(cx, cy, a, R_SLOT, H2))
        pts.append(_pt(cx, cy, a, R_ROOT, H_ROOT))
    return pts


def finger_points(cx, cy, k):
    """Finger between slot k and slot k+1: bounded by the two slot walls,
    the core flat and the hull chord joining the two slot-end corners."""
    a0 = k * DA
    a1 = a0 + DA
    return [
        _pt(cx, cy, a0, R_ROOT, H_ROOT),
        _pt(cx, cy, a0, R_SLOT, H2),
        _pt(cx, cy, a1, R_SLOT, -H2),
        _pt(cx, cy, a1, R_ROOT, -H_ROOT),
    ]


# every star: (centre x, centre y, list of finger sectors that lie inside the bar)
stars = [(x, 0.0, list(range(N_SLOTS))) for x in centre_x]
for x in edge_x:
    stars.append((x, -W / 2.0, list(range(0, N_SLOTS // 2))))        # front edge, fingers point +Y
    stars.append((x, W / 2.0, list(range(N_SLOTS // 2, N_SLOTS))))   # back edge, fingers point -Y

# ---------------- top plate with the star holes ----------------
plate = cq.Workplane("XY").box(L, W, T, centered=(True, True, False)).translate((0, 0, -T))

cut_wp = cq.Workplane("XY", origin=(0, 0, -T - 1.0))
for (sx, sy, _) in stars:
    cut_wp = cut_wp.polyline(star_points(sx, sy)).close()
star_cutters = cut_wp.extrude(T + 2.0)
plate = plate.cut(star_cutters)

# ---------------- fingers hanging below the plate ----------------
fing_wp = cq.Workplane("XY", origin=(0, 0, -H))
for (sx, sy, sectors) in stars:
    for k in sectors:
        fing_wp = fing_wp.polyline(finger_points(sx, sy, k)).close()
fingers = fing_wp.extrude(H - T)

result = plate.union(fingers)
